import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
TOTAL_LEN = 550.0      # overall length, tip to tip (X)
CLV_H = 25.0           # clevis height (Z)
CLV_W = 42.2           # clevis outer width (Y)
CLV_L = 58.0           # clevis length from base outer face to prong tip (X)
WALL = 7.4             # prong thickness
BASE_WALL = 6.7        # thickness of the fork base (X)
R_OUT = 8.0            # outer radius of the U corners
PIN_D = 12.0           # cross hole through the prongs
PIN_FROM_TIP = 12.2    # cross hole centre measured from prong tip
TUBE_OD = 24.5         # connecting tube
TUBE_ID = 20.0
VENT_D = 6.3           # two axial holes in each clevis base
VENT_Z = 6.2           # their offset above / below the axis
VENT_CB_D = 7.5        # shallow counterbore on the fork side of the axial holes
VENT_CB_DEPTH = 0.4

SEAM_ANGLE = -50.0      # angular position of the tube surface seam (cosmetic only)

VIEW = {"azimuth": 45, "elevation": 26}

x_base = TOTAL_LEN / 2.0 - CLV_L   # base outer face of the +X clevis


def make_clevis():
    """U-shaped fork at the +X end, opening toward +X."""
    outer = (
        cq.Workplane("XY")
        .box(CLV_L, CLV_W, CLV_H, centered=(False, True, True))
        .translate((x_base, 0, 0))
        .edges("|Z and <X")
        .fillet(R_OUT)
    )
    slot_len = CLV_L - BASE_WALL
    inner = (
        cq.Workplane("XY")
        .box(slot_len + 5.0, CLV_W - 2 * WALL, CLV_H + 2.0, centered=(False, True, True))
        .translate((x_base + BASE_WALL, 0, 0))
    )
    fork = outer.cut(inner)
    # cross (pin) hole through both prongs
    x_pin = TOTAL_LEN / 2.0 - PIN_FROM_TIP
    pin = (
        cq.Workplane("XZ")
        .center(x_pin, 0)
        .circle(PIN_D / 2.0)
        .extrude(CLV_W, both=True)
    )
    fork = fork.cut(pin)
    # two axial holes through the base, counterbored on the inside of the fork
    for z in (VENT_Z, -VENT_Z):
        h = (
            cq.Workplane("YZ")
            .workplane(offset=x_base - 1.0)
            .center(0, z)
            .circle(VENT_D / 2.0)
            .extrude(BASE_WALL + 2.0)
        )
        cb = (
            cq.Workplane("YZ")
            .workplane(offset=x_base + BASE_WALL - VENT_CB_DEPTH)
            .center(0, z)
            .circle(VENT_CB_D / 2.0)
            .extrude(VENT_CB_DEPTH + 1.0)
        )
        fork = fork.cut(h).cut(cb)
    return fork


clevis_r = make_clevis()
clevis_l = clevis_r.mirror("YZ")

tube = (
    cq.Workplane("YZ")
    .workplane(offset=-x_base - 0.5)
    .circle(TUBE_OD / 2.0)
    .circle(TUBE_ID / 2.0)
    .extrude(2 * x_base + 1.0)
    .rotate((0, 0, 0), (1, 0, 0), SEAM_ANGLE)  # park the cylinder seam on the back-bottom side
)

result = clevis_r.union(tube).union(clevis_l)
